import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
D = 70.0            # body outer diameter
R = D / 2.0
H = 114.8           # height of the can from the bottom rim to the top of the lip
NECK_H = 12.7       # lip top down to the bead centre
NECK_BASE_INSET = 0.0   # neck radius just above the bead, inset from the body
NECK_TOP_INSET = 1.9    # neck radius at the lip, inset from the body (tapered neck)
BEAD_PROUD = 0.75   # how far the bead stands out of the body
BEAD_HALF = 1.3     # half height of the bead
WALL = 1.0          # wall thickness of the body (side and bottom)
LIP_WALL = 2.2      # wall thickness at the lip: the neck wall thickens upwards
RIM_FILLET = 1.4    # outer rounding of the lip
DOME_H = 1.5        # the bottom bulges out as a shallow dome ...
DOME_N = 4          # ... flat in the middle, curving up towards the rim
TILT = 16.6         # tilt of the can axis about X (top leans to +Y)
SEAM_ANGLE = 225.0  # where the revolve seam sits around the axis

# small loose strip floating above the can
STRIP_L = 8.2
STRIP_W = 0.8
STRIP_T = 0.25
STRIP_POS = (22.8, 50.5, 169.1)

zb = H - NECK_H
Rn0 = R - NECK_BASE_INSET
Rn1 = R - NECK_TOP_INSET

# ---------------- can wall: one revolved cross-section ----------------
# outside: body, rolled bead, tapered neck; inside: bore, groove behind the
# bead, and a conical mouth that flares out downwards into the bore.
Ri = R - WALL                 # body bore radius
Ri_top = Rn1 - LIP_WALL       # bore radius at the lip
body = (
    cq.Workplane("XZ")
    .moveTo(0, 0)
    .lineTo(R, 0)
    .lineTo(R, zb - BEAD_HALF)
    .threePointArc((R + BEAD_PROUD, zb), (Rn0, zb + BEAD_HALF))
    .lineTo(Rn1, H)
    .lineTo(Ri_top, H)
    .lineTo(Ri, zb + BEAD_HALF)
    .threePointArc((R + BEAD_PROUD - WALL, zb), (Ri, zb - BEAD_HALF))
    .lineTo(Ri, WALL)
    .lineTo(0, WALL)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)

# domed bottom: the underside bulges out as a smooth, flat-centred dome
# z = -DOME_H * (1 - (r / r0) ** DOME_N).  Built as one untrimmed spline
# surface (no seam, no poles) that splits a thin disc; the piece between the
# surface and the bottom plane is the dome.
r0 = R - 0.15
def dome_z(x, y):
    return -DOME_H * (1.0 - (math.hypot(x, y) / r0) ** DOME_N)

n_grid = 15
span = R + 3.0
grid = [-span + 2.0 * span * i / (n_grid - 1) for i in range(n_grid)]
dome_face = cq.Face.makeSplineApprox(
    [[cq.Vector(x, y, dome_z(x, y)) for y in grid] for x in grid], tol=1e-3, minDeg=2, maxDeg=5
)
disc = cq.Solid.makeCylinder(R, DOME_H + 1.0, cq.Vector(0, 0, -DOME_H - 1.0))
pieces = disc.split(dome_face).Solids()
dome = cq.Workplane("XY").add(max(pieces, key=lambda p: p.Center().z))

can = body.union(dome, clean=True)

# round the outer lip edge
can = can.edges(
    cq.selectors.BoxSelector((-R - 1, -R - 1, H - 0.01), (R + 1, R + 1, H + 0.01))
).edges(cq.selectors.RadiusNthSelector(1)).fillet(RIM_FILLET)

# park the seam of the revolved faces on a silhouette, then tilt the whole can
can = can.rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE).rotate((0, 0, 0), (1, 0, 0), -TILT)

strip = (
    cq.Workplane("XY")
    .box(STRIP_W, STRIP_L, STRIP_T)
    .rotate((0, 0, 0), (1, 0, 0), -TILT)
    .translate(STRIP_POS)
)

result = can.union(strip)
